import math
import cadquery as cq

# ======================================================================
#  Block with an inclined guide ridge.
#  A 14 mm bore runs at 15 deg from the middle of the +X end face up and
#  out through the slanted end face of a rounded ridge that sits on the
#  block top.  The ridge is a rounded square bar around that bore axis; its
#  sloping top blends (and flares out) into the block top near the +X end.
# ======================================================================

# ---------------- driving dimensions (mm) ----------------
L = 86.0          # block length (X)
W = 37.0          # block width (Y)
H = 30.0          # block height (Z)
EDGE_R = 2.0      # rounds on block top edges and +X vertical edges

FL_LEN = 5.0      # lip (flange) at the -X end, length in X
FL_H = 5.0        # lip height

TILT = 15.0       # inclination of bore / ridge (deg)
BORE_D = 14.0     # inclined through bore
BORE_Z = H / 2.0  # bore axis height at the +X end face

RIDGE_HW = 12.0   # ridge half width (= half size of the bar around the bore)
RIDGE_TOP = 12.0  # ridge top, perpendicular distance above the bore axis
RIDGE_TOP_R = 4.5   # rounds on the ridge top edges and its end
RIDGE_BASE_R = 4.45 # blend between ridge and block top

FLARE_X0 = 57.0   # flat ridge top starts to widen here
FLARE_OVER = 3.0  # flare loft runs this far past the pad line (buried)
FLARE_K = 0.0185  # top half width grows as k*(x-FLARE_X0)^2
FLARE_N = 4       # loft sections in the flare

TAP_END_D = 9.0   # tapped hole in the -X end face (plain, no thread)
TAP_END_Z = H / 2.0
TAP_END_DEPTH = 16.0

TAP_BOT_D = 11.0  # tapped hole from the bottom, breaking into the bore
TAP_BOT_X = L - 24.8

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived geometry ----------------
a = math.radians(TILT)
slope = math.tan(a)
axis_dir = (-math.cos(a), math.sin(a))  # bore direction (x, z), towards -X / up
T = cq.Vector(math.cos(a), 0, -math.sin(a))  # along the ridge, towards +X (down)
U = cq.Vector(math.sin(a), 0, math.cos(a))   # ridge "up" (normal of sloped top)
O = cq.Vector(0, 0, H)                       # lower edge of the slanted end face


def bore_axis_z(x):
    return BORE_Z + slope * (L - x)


# ridge frame: s along T from the end face, n along U
N_AXIS = (cq.Vector(L, 0, BORE_Z) - O).dot(U)   # bore axis height in the frame
N_TOP = N_AXIS + RIDGE_TOP                      # sloped top of the ridge
N_BOT = -6.0                                    # ridge bottom (buried / clipped)
S_PAD = N_TOP / math.tan(a)                     # sloped top meets block top


def s_of_top_x(x):
    # s of the point on the ridge top whose x coordinate is x
    return (x - N_TOP * math.sin(a)) / math.cos(a)


S_FLARE0 = s_of_top_x(FLARE_X0)
S_FLARE1 = S_PAD + FLARE_OVER
RIDGE_END = (O + T * S_PAD + U * N_TOP).x      # where top meets block (~76.4)
CLIP_HW = W / 2 - EDGE_R - 0.05

# ---------------- main block ----------------
block = cq.Workplane("XY").box(L, W, H, centered=(False, True, False))
block = block.edges("|X and >Z").fillet(EDGE_R)
block = block.edges(">X and (not <Z)").fillet(EDGE_R)


# ---------------- ridge ----------------
def ridge_plane(s):
    return cq.Plane(origin=O + T * s, xDir=(0, 1, 0), normal=T)


def ridge_section(s, hw, rt=RIDGE_TOP_R):
    """Rounded-top rectangle perpendicular to the ridge (local x = Y, y = n)."""
    c = math.cos(math.radians(45))
    wp = (
        cq.Workplane(ridge_plane(s))
        .moveTo(-hw, N_BOT)
        .lineTo(hw, N_BOT)
        .lineTo(hw, N_TOP - rt)
        .threePointArc((hw - rt + rt * c, N_TOP - rt + rt * c), (hw - rt, N_TOP))
        .lineTo(-hw + rt, N_TOP)
        .threePointArc((-hw + rt - rt * c, N_TOP - rt + rt * c), (-hw, N_TOP - rt))
        .close()
    )
    return wp.wires().val()


def flare_top_hw(s):
    k = FLARE_K * math.cos(a) ** 2
    return (RIDGE_HW - RIDGE_TOP_R) + k * max(0.0, s - S_FLARE0) ** 2


# straight part: rounded bar along the bore with a rounded end (slanted face)
bar = (
    cq.Workplane(ridge_plane(0.0))
    .rect(2 * RIDGE_HW, N_TOP - N_BOT, centered=(True, False))
    .extrude(S_FLARE0)
    .translate(U * N_BOT)
)
bar_solid = bar.val()


def _bar_edge(e):
    c = e.Center() - O
    s, n = c.dot(T), c.dot(U)
    top_long = abs(n - N_TOP) < 1e-4 and abs(abs(c.y) - RIDGE_HW) < 1e-4
    end = abs(s) < 1e-4 and n > N_BOT + 1e-3
    return top_long or end


bar_solid = bar_solid.fillet(RIDGE_TOP_R, [e for e in bar_solid.Edges() if _bar_edge(e)])

# flare part: flat ridge top widens towards the +X end
fs = [S_FLARE0 + i * (S_FLARE1 - S_FLARE0) / (FLARE_N - 1) for i in range(FLARE_N)]
flare = cq.Solid.makeLoft(
    [ridge_section(s, flare_top_hw(s) + RIDGE_TOP_R) for s in fs], False
)
ridge = cq.Workplane().add(bar_solid.fuse(flare).clean())

clip = cq.Workplane("XY").box(L, 2 * CLIP_HW, H + 40, centered=(False, True, False))
ridge = ridge.intersect(clip)

body = block.union(ridge)


# blend between ridge and block top
def _base_edge(e):
    bb = e.BoundingBox()
    return (abs(bb.zmin - H) < 1e-3 and abs(bb.zmax - H) < 1e-3
            and bb.xmin > 0.05 and bb.xmax < L - EDGE_R - 0.5
            and bb.ymin > -W / 2 + EDGE_R + 0.2 and bb.ymax < W / 2 - EDGE_R - 0.2)


base_edges = [e for e in body.val().Edges() if _base_edge(e)]
body = body.newObject([body.val().fillet(RIDGE_BASE_R, base_edges)])

# ---------------- lip at -X end ----------------
lip = (
    cq.Workplane("XY")
    .box(FL_LEN, W, FL_H, centered=(False, True, False))
    .translate((-FL_LEN, 0, 0))
)
body = body.union(lip)

# ---------------- holes ----------------
# inclined through bore: from the +X face centre up through the ridge end face
bore_len = 140.0
start = (L + 30 * math.cos(a), BORE_Z - 30 * math.sin(a))
bore = cq.Solid.makeCylinder(
    BORE_D / 2, bore_len,
    cq.Vector(start[0], 0, start[1]), cq.Vector(axis_dir[0], 0, axis_dir[1])
)
body = body.cut(cq.Workplane().add(bore))

# tapped hole in the -X end face
tap_end = (
    cq.Workplane("YZ").center(0, TAP_END_Z).circle(TAP_END_D / 2).extrude(TAP_END_DEPTH)
)
body = body.cut(tap_end)

# tapped hole from the bottom, up into the bore
tap_bot = (
    cq.Workplane("XY").center(TAP_BOT_X, 0).circle(TAP_BOT_D / 2)
    .extrude(bore_axis_z(TAP_BOT_X))
)
body = body.cut(tap_bot)

result = body
